import math
import cadquery as cq

# ---------------- main dimensions (mm) ----------------
L = 100.0          # length  (X)
W = 44.4           # width   (Y)
H = 34.7           # height  (Z)
R_CORNER = 4.0     # vertical corner radius of the top cap
R_WALL = 4.0       # vertical corner radius of the walls below the cap
T_WALL = 2.0       # side wall thickness
T_TOP = 2.4        # top plate thickness
PAD_T = 1.6        # extra thickness under the grooved corner
R_INNER = 4.0      # inner vertical corner radius of the cavity
CAP_H = 2.5        # height of the top cap band
CAP_STEP = 0.15    # cap overhang over the right-end wall
TOP_FILLET = 0.0   # top outer edge fillet (sharp)

# top features
HOLE_L, HOLE_W = 7.5, 6.2          # elliptical mounting holes at left end
HOLE_X, HOLE_Y = -41.8, 12.45
SLOT_X0, SLOT_X1 = -34.4, -14.4    # rectangular slot on top
SLOT_Y0, SLOT_Y1 = -17.0, -9.0
BOOT_X, BOOT_Y, BOOT_D = 30.0, 2.3, 5.5
BOOT_BOSS_D, BOOT_BOSS_Z0 = 8.0, 29.6      # button guide tube under the top plate

# C64 logo (oval pocket with raised letters and bars)
LOGO_X, LOGO_Y = -5.7, 1.1
LOGO_LEN, LOGO_H, LOGO_DEPTH = 37.4, 9.9, 1.0
LETTER_H, LETTER_W, LETTER_SW = 8.0, 6.3, 1.3
C_X, SIX_X, FOUR_X = 2.35, -5.4, -13.0       # letter centres (world X)
BAR_PITCH, BAR_W, BAR_N = 1.7, 0.85, 5

# "Boot" engraving
BOOTTXT_X, BOOTTXT_Y, BOOTTXT_DEPTH = 38.5, 11.9, 0.7   # outer edge of "B" / baseline
BT_CAP, BT_STROKE, BT_B_W = 6.4, 1.25, 5.0
BT_O_D, BT_O_U = 4.5, (7.7, 12.5)
BT_T_U, BT_T_H = 16.3, 5.9

# diagonal sawtooth grooves at the front-right top corner
GROOVE_ANG = 41.9
GROOVE_N = 6
GROOVE_FIRST = 7.1
GROOVE_PITCH = 3.62
GROOVE_W = 2.0
GROOVE_D = 2.5

# right end (+X)
RS_Y, RS_Z, RS_LEN, RS_H = -6.6, 27.4, 15.8, 5.8     # stadium slot
NOTCH_Y0, NOTCH_Y1, NOTCH_Z, NOTCH_R = -12.8, 13.3, 20.1, 1.4

# left end (-X)
LS_Y, LS_Z, LS_LEN, LS_H = 0.1, 11.8, 16.6, 6.0
LR_Y, LR_Z, LR_LEN, LR_H = -2.1, 5.35, 21.5, 2.1

# back wall (+Y) D-sub
DSUB_X, DSUB_Z = -9.0, 19.6
DSUB_TOP, DSUB_BOT, DSUB_H, DSUB_R = 33.0, 27.0, 20.0, 2.8
DSUB_HOLE_SP, DSUB_HOLE_D = 43.6, 4.0

# interior
BOSS_X1, BOSS_Y0, BOSS_Z0 = -37.7, 7.6, 16.3        # corner screw bosses
HOUSE_X0, HOUSE_X1, HOUSE_Y0, HOUSE_Y1, HOUSE_Z0 = -35.6, -13.2, -18.2, -7.9, 13.1
SHELF_X0, SHELF_Y0, SHELF_Z0, SHELF_T = 21.0, 5.5, 20.1, 1.8
BLOCK_X0 = 43.0                                     # block above the shelf at the end wall
PIN_X, PIN_Z, PIN_D, PIN_DEPTH = 33.8, 1.5, 2.2, 1.2

ZTOP_IN = H - T_TOP
XI, YI = L / 2 - T_WALL, W / 2 - T_WALL        # inner wall faces


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------- body shell ----------------
# the walls below the cap are set back slightly at the right (+X) end only
walls = (cq.Workplane("XY").center(-CAP_STEP / 2, 0).rect(L - CAP_STEP, W).extrude(H - CAP_H)
         .edges("|Z").fillet(R_WALL))
cap = (cq.Workplane("XY").workplane(offset=H - CAP_H).rect(L, W).extrude(CAP_H)
       .edges("|Z").fillet(R_CORNER))
if TOP_FILLET > 0:
    cap = cap.faces(">Z").edges().fillet(TOP_FILLET)
outer = walls.union(cap)
cavity = (cq.Workplane("XY").workplane(offset=-1).rect(2 * XI, 2 * YI)
          .extrude(ZTOP_IN + 1).edges("|Z").fillet(R_INNER))
body = outer.cut(cavity)

# ---------------- interior bosses / housing / shelf ----------------
for sgn in (1, -1):
    y0, y1 = sorted((sgn * BOSS_Y0, sgn * (YI + 0.5)))
    body = body.union(box(-XI - 0.5, BOSS_X1, y0, y1, BOSS_Z0, ZTOP_IN + 0.5))
body = body.union(box(HOUSE_X0, HOUSE_X1, HOUSE_Y0, HOUSE_Y1, HOUSE_Z0, ZTOP_IN + 0.5))
body = body.union(box(SHELF_X0, XI + 0.5, SHELF_Y0, YI + 0.5, SHELF_Z0, SHELF_Z0 + SHELF_T))
body = body.union(box(BLOCK_X0, XI + 0.5, SHELF_Y0, YI + 0.5, SHELF_Z0, ZTOP_IN + 0.5))

# ---------------- top features ----------------
top = cq.Workplane("XY").workplane(offset=H)
holes = (top.pushPoints([(HOLE_X, HOLE_Y), (HOLE_X, -HOLE_Y)])
         .ellipse(HOLE_L / 2, HOLE_W / 2).extrude(-(H - BOSS_Z0) - 1, both=True))
body = body.cut(holes)

rslot = (cq.Workplane("XY").workplane(offset=HOUSE_Z0 - 1)
         .center((SLOT_X0 + SLOT_X1) / 2, (SLOT_Y0 + SLOT_Y1) / 2)
         .rect(SLOT_X1 - SLOT_X0, SLOT_Y1 - SLOT_Y0).extrude(H - HOUSE_Z0 + 2)
         .edges("|Z").fillet(1.0))
body = body.cut(rslot)

bguide = (cq.Workplane("XY").workplane(offset=BOOT_BOSS_Z0).center(BOOT_X, BOOT_Y)
          .circle(BOOT_BOSS_D / 2).extrude(ZTOP_IN - BOOT_BOSS_Z0 + 0.5))
body = body.union(bguide)
boot = (cq.Workplane("XY").workplane(offset=BOOT_BOSS_Z0 - 1).center(BOOT_X, BOOT_Y)
        .circle(BOOT_D / 2).extrude(H - BOOT_BOSS_Z0 + 2))
body = body.cut(boot)

# --- C64 logo: oval pocket leaving raised letters and bars ---
# local frame: u reads toward -X, v (letter "up") points toward -Y
logo_pl = cq.Plane(origin=(LOGO_X, LOGO_Y, H - LOGO_DEPTH), xDir=(-1, 0, 0), normal=(0, 0, 1))


def lw():
    return cq.Workplane(logo_pl)


EXT = LOGO_DEPTH + 1.0
pocket = lw().slot2D(LOGO_LEN, LOGO_H, 0).extrude(EXT)

hl = LETTER_H / 2
sw = LETTER_SW
lw_w = LETTER_W


def ring_letter(uc):
    o = lw().center(uc, 0).slot2D(LETTER_H, lw_w, 90).extrude(EXT)
    i = lw().center(uc, 0).slot2D(LETTER_H - 2 * sw, lw_w - 2 * sw, 90).extrude(EXT)
    return o.cut(i)


uc_, u6_, u4_ = LOGO_X - C_X, LOGO_X - SIX_X, LOGO_X - FOUR_X
# "C"
c_l = ring_letter(uc_).cut(lw().center(uc_ + 2.2, 0).rect(4.4, 3.4).extrude(EXT))
# "6"
six = ring_letter(u6_)
six = six.cut(lw().center(u6_ + 1.7, 2.0).rect(3.4, 1.7).extrude(EXT))
six = six.union(lw().center(u6_, 0.5).rect(lw_w - 0.4, sw).extrude(EXT))
# "4"
four = lw().center(u4_ + 1.3, 0).rect(sw, LETTER_H).extrude(EXT)
four = four.union(lw().center(u4_ - 0.1, -2.45).rect(lw_w + 0.6, sw).extrude(EXT))
four = four.union(lw().polyline([(u4_ - 3.4, -3.1), (u4_ - 1.6, -3.1), (u4_ + 0.7, 2.4),
                                 (u4_ + 0.7, hl), (u4_ - 0.1, hl)]).close().extrude(EXT))
raised = c_l.union(six).union(four)

# bars at both ends of the oval
inner_oval = lw().slot2D(LOGO_LEN - 1.2, LOGO_H - 1.2, 0).extrude(EXT)
for k in range(BAR_N):
    v = (k - (BAR_N - 1) / 2) * BAR_PITCH
    for u0 in (u4_ + lw_w / 2 + 0.5, uc_ - lw_w / 2 - 0.5):
        side = 1 if u0 > 0 else -1
        ua, ub = abs(u0), LOGO_LEN / 2
        bar = lw().center(side * (ua + ub) / 2, v).rect(ub - ua, BAR_W).extrude(EXT)
        raised = raised.union(bar.intersect(inner_oval))
pocket = pocket.cut(raised)
body = body.cut(pocket)

# --- "Boot" engraving (reads from the back side) ---
# local frame: u from the outer edge of the "B" toward -X, v from the baseline toward -Y
bt_pl = cq.Plane(origin=(BOOTTXT_X, BOOTTXT_Y, H - BOOTTXT_DEPTH), xDir=(-1, 0, 0),
                 normal=(0, 0, 1))


def bw():
    return cq.Workplane(bt_pl)


E2 = BOOTTXT_DEPTH + 1.0
st = BT_STROKE
capH = BT_CAP


def dshape(u0, vb, vt, w):
    """solid 'D' shaped letter part with a counter: stem at u0, total width w"""
    r = (vt - vb) / 2
    o = (bw().center(u0 + (w - r) / 2, (vb + vt) / 2).rect(w - r, vt - vb).extrude(E2)
         .union(bw().center(u0 + w - r, (vb + vt) / 2).circle(r).extrude(E2)))
    ri = r - st
    i = (bw().center(u0 + st + (w - r - st) / 2, (vb + vt) / 2).rect(w - r - st, 2 * ri).extrude(E2)
         .union(bw().center(u0 + w - r, (vb + vt) / 2).circle(ri).extrude(E2)))
    return o.cut(i)


vm = capH * 0.5
letters = dshape(0.0, 0.0, vm + 0.5 * st, BT_B_W).union(dshape(0.0, vm - 0.5 * st, capH, BT_B_W - 0.4))
xr = BT_O_D / 2
for uo in BT_O_U:
    ring = (bw().center(uo, xr).circle(xr).extrude(E2)
            .cut(bw().center(uo, xr).circle(xr - st).extrude(E2)))
    letters = letters.union(ring)
ut = BT_T_U
letters = letters.union(bw().center(ut, st / 2 + (BT_T_H - st) / 2).rect(st, BT_T_H - st).extrude(E2))
letters = letters.union(bw().center(ut + 0.45, BT_O_D - 0.45).rect(3.4, st * 0.9).extrude(E2))
letters = letters.union(bw().center(ut + 0.9, st / 2).rect(1.8 + st, st).extrude(E2))
body = body.cut(letters)

# --- sawtooth grooves ---
th = math.radians(GROOVE_ANG)
dx, dy = math.cos(th), math.sin(th)       # groove direction
nx, ny = math.sin(th), -math.cos(th)      # toward the corner
cx, cy = L / 2, -W / 2
# pad under the grooved corner so the grooves do not break through the thin top plate
s_pad = GROOVE_FIRST + GROOVE_N * GROOVE_PITCH + 1.0
pad_pts = [(cx, cy), (cx - s_pad / nx, cy), (cx, cy + s_pad / (-ny))]
pad = (cq.Workplane("XY").workplane(offset=ZTOP_IN - PAD_T).polyline(pad_pts).close()
       .extrude(PAD_T + 0.5))
body = body.union(pad.intersect(cavity))
for i in range(GROOVE_N):
    s_wall = GROOVE_FIRST + i * GROOVE_PITCH      # vertical wall distance from corner
    s_in = s_wall + GROOVE_W
    pts = [(s_wall, H + 1.0), (s_wall, H - GROOVE_D), (s_in, H), (s_in + 1.0, H + 1.0)]
    pl = cq.Plane(origin=(cx, cy, 0), xDir=(-nx, -ny, 0), normal=(dx, dy, 0))
    prism = cq.Workplane(pl).polyline(pts).close().extrude(80, both=True)
    body = body.cut(prism)

# ---------------- right end (+X) ----------------
rend = cq.Workplane("YZ").workplane(offset=L / 2)
rs = rend.center(RS_Y, RS_Z).slot2D(RS_LEN, RS_H, 0).extrude(-6, both=True)
body = body.cut(rs)
notch = (cq.Workplane("YZ").workplane(offset=L / 2 - 6)
         .center((NOTCH_Y0 + NOTCH_Y1) / 2, (NOTCH_Z - 3) / 2)
         .rect(NOTCH_Y1 - NOTCH_Y0, NOTCH_Z + 3).extrude(12)
         .edges("|X").fillet(NOTCH_R))
body = body.cut(notch)

# ---------------- left end (-X) ----------------
lend = cq.Workplane("YZ").workplane(offset=-L / 2)
ls = lend.center(LS_Y, LS_Z).slot2D(LS_LEN, LS_H, 0).extrude(-6, both=True)
body = body.cut(ls)
lr = lend.center(LR_Y, LR_Z).rect(LR_LEN, LR_H).extrude(-6, both=True)
body = body.cut(lr)

# ---------------- back wall D-sub ----------------
back = cq.Workplane("XZ", origin=(0, W / 2, 0))
ht, hb, hh = DSUB_TOP / 2, DSUB_BOT / 2, DSUB_H / 2
dpts = [(-ht, hh), (ht, hh), (hb, -hh), (-hb, -hh)]
dsub = (back.center(DSUB_X, DSUB_Z).polyline(dpts).close().extrude(-6, both=True)
        .edges("|Y").fillet(DSUB_R))
body = body.cut(dsub)
dh = (back.pushPoints([(DSUB_X - DSUB_HOLE_SP / 2, DSUB_Z), (DSUB_X + DSUB_HOLE_SP / 2, DSUB_Z)])
      .circle(DSUB_HOLE_D / 2).extrude(-6, both=True))
body = body.cut(dh)

# small blind pin holes near the bottom of the long walls (lid catches)
for sy in (1, -1):
    for sx in (1, -1):
        pin = (cq.Workplane("XZ", origin=(0, sy * YI, 0))
               .center(sx * PIN_X, PIN_Z).circle(PIN_D / 2).extrude(PIN_DEPTH, both=True))
        body = body.cut(pin)

result = body
